import math
import cadquery as cq

# ---------------------------------------------------------------
# Bell-crank / clevis lever  (all dimensions in mm)
#   - big end  B : clevis (upper tine + lower tine with a slot between)
#   - boss     O : central pivot boss, raised above the upper tine
#   - small end S: arm at mid height, chamfered underneath
# ---------------------------------------------------------------
K = 0.4  # design-unit -> mm  (design sketched in units, 1 unit = 0.4 mm)

# pivot centres in plan (XY)
BX, BY = -39.3 * K, -86.3 * K      # big (clevis) end
SX, SY = 71.5 * K, 104.0 * K       # small end
OX, OY = 0.0, 0.0                  # central boss

R_BOSS = 31.0 * K        # central boss radius
R_UP_END = 26.5 * K      # upper clevis tine end radius
R_LOW_END = 17.4 * K     # lower tine end radius
R_SMALL = 18.9 * K       # small end radius

# common flat front face (vertical plane), direction in plan, tangent
# to the lower tine end
FRONT_DIR = 58.0         # deg
UP_FRONT_DIR = 71.5      # deg, upper tine front flat (tangent to big end)

# flanks of the small arm: big concave arcs tangent to the boss and
# to a virtual circle at the small end  (radius, virtual end radius)
ARM_BACK_R, ARM_BACK_RV = 354.0 * K, 14.2 * K
ARM_FRONT_R, ARM_FRONT_RV = 497.0 * K, 16.7 * K

# heights
Z_BOT = 0.0
Z_ARM_BOT = 50.5 * K     # underside of the small-end arm
Z_TINE_TOP = 66.0 * K    # top of lower clevis tine (slot floor)
Z_MID = 96.0 * K         # slot roof / arm top
Z_UP_TOP = 121.0 * K     # top of upper tine
Z_TOP = 125.0 * K        # top of boss

# holes
R_HOLE = 10.0 * K
R_HOLE_SMALL = 9.5 * K
R_CBORE = 19.7 * K
CBORE_DEPTH = 15.0 * K
R_CSK_LOW = 14.6 * K
F_BOSS_HOLE = 2.8 * K

# slot back wall (45 deg to B-S axis) : along - perp = WALL_C
WALL_C = 35.5 * K
# inclined cut under the small arm (along B-S axis from B)
CH_A0 = 137.0 * K
CH_A1 = 174.0 * K

F_SMALL = 8.0 * K        # plan fillet small end / arm flanks
F_WAIST = 40.0 * K       # plan blend upper tine front / FP
F_WAIST_B = 15.0 * K     # plan blend big end / upper tine back
F_BOSS_UP = 3.5 * K      # boss to upper tine top
F_BOSS_ARM = 12.0 * K    # boss to arm top
F_WALL_BACK = 11.0 * K   # vertical round, slot wall / back flank
F_WALL_FRONT = 5.0 * K   # vertical round, slot wall / front face

# ---------------------------------------------------------------
# helpers
# ---------------------------------------------------------------
ux, uy = SX - BX, SY - BY
L_BS = math.hypot(ux, uy)
ux, uy = ux / L_BS, uy / L_BS          # axis B->S
nx, ny = uy, -ux                       # "front" normal (right of axis)

L_OS = math.hypot(SX - OX, SY - OY)
vx, vy = (SX - OX) / L_OS, (SY - OY) / L_OS   # axis O->S
mx, my = vy, -vx                               # front normal of O->S

Bc, Oc, Sc = (BX, BY), (OX, OY), (SX, SY)


def frame(a, p):
    """B-S frame (along, perp) -> XY"""
    return (BX + a * ux + p * nx, BY + a * uy + p * ny)


def frame_os(a, p):
    """O-S frame (along, perp) -> XY"""
    return (OX + a * vx + p * mx, OY + a * vy + p * my)


def add(p, q, s=1.0):
    return (p[0] + s * q[0], p[1] + s * q[1])


def dot(p, q):
    return p[0] * q[0] + p[1] * q[1]


def unit(c, p):
    d = math.hypot(p[0] - c[0], p[1] - c[1])
    return ((p[0] - c[0]) / d, (p[1] - c[1]) / d)


def ang(c, p):
    return math.atan2(p[1] - c[1], p[0] - c[0])


def on_circ(c, r, t):
    return (c[0] + r * math.cos(t), c[1] + r * math.sin(t))


def arc_mid(c, r, p0, p1, ccw):
    t0, t1 = ang(c, p0), ang(c, p1)
    if ccw:
        dt = (t1 - t0) % (2 * math.pi)
        return on_circ(c, r, t0 + dt / 2)
    dt = (t0 - t1) % (2 * math.pi)
    return on_circ(c, r, t0 - dt / 2)


def tangent_normal(c1, r1, c2, r2, side):
    """unit normal of the external tangent of two circles.
    side=+1 : right of c1->c2 (front), -1 : left (back)"""
    (x1, y1), (x2, y2) = c1, c2
    dx, dy = x2 - x1, y2 - y1
    L = math.hypot(dx, dy)
    ex, ey = dx / L, dy / L
    px, py = ey, -ex
    s = (r1 - r2) / L
    c = math.sqrt(1 - s * s)
    return (ex * s + side * px * c, ey * s + side * py * c)


def circle_circle(c1, r1, c2, r2, pick):
    """intersection of two circles, choose point with max dot(pick)"""
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dy)
    a = (r1 * r1 - r2 * r2 + d * d) / (2 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    bx, by = c1[0] + a * dx / d, c1[1] + a * dy / d
    p1 = (bx + h * dy / d, by - h * dx / d)
    p2 = (bx - h * dy / d, by + h * dx / d)
    return p1 if dot(p1, pick) > dot(p2, pick) else p2


def line_circle(c_line, n, cc, r, pick):
    """intersection of line n.x = c_line with circle(cc, r)"""
    t = (-n[1], n[0])
    foot = (n[0] * c_line, n[1] * c_line)
    fx, fy = foot[0] - cc[0], foot[1] - cc[1]
    b = fx * t[0] + fy * t[1]
    cc_ = fx * fx + fy * fy - r * r
    disc = math.sqrt(max(b * b - cc_, 0.0))
    p1 = (foot[0] + (-b + disc) * t[0], foot[1] + (-b + disc) * t[1])
    p2 = (foot[0] + (-b - disc) * t[0], foot[1] + (-b - disc) * t[1])
    return p1 if dot(p1, pick) > dot(p2, pick) else p2


def concave_arc_centre(R, r1, r2, side):
    """centre (O-S frame) of a circle of radius R touching circle(O,r1)
    and circle(S,r2) from outside, on side +1 (front) / -1 (back)"""
    d1, d2 = R + r1, R + r2
    a = (d1 * d1 - d2 * d2 + L_OS * L_OS) / (2 * L_OS)
    h = math.sqrt(d1 * d1 - a * a)
    return (a, side * h)


def closed(pts):
    return list(pts) + [pts[0]]


def slab(sketch, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .placeSketch(sketch).extrude(z1 - z0))


def near(p):
    return cq.selectors.NearestToPointSelector((p[0], p[1], 0))


# ---------------------------------------------------------------
# plan geometry
# ---------------------------------------------------------------
# front plane FP : nF . x = cF
nF = (math.cos(math.radians(FRONT_DIR - 90.0)), math.sin(math.radians(FRONT_DIR - 90.0)))
cF = dot(nF, Bc) + R_LOW_END
dirF = (-nF[1], nF[0])

# back flank of the lower body: tangent lower end -> boss
nB1 = tangent_normal(Bc, R_LOW_END, Oc, R_BOSS, -1)
cB1 = dot(nB1, Bc) + R_LOW_END

# small arm flanks (concave arcs)
cb_a, cb_p = concave_arc_centre(ARM_BACK_R, R_BOSS, ARM_BACK_RV, -1)
CB = frame_os(cb_a, cb_p)
cf_a, cf_p = concave_arc_centre(ARM_FRONT_R, R_BOSS, ARM_FRONT_RV, +1)
CF = frame_os(cf_a, cf_p)
dS = (-vx, -vy)

# key points of the lower body outline
t_b_f = add(Bc, nF, R_LOW_END)                       # FP tangent on lower end
i_f1 = line_circle(cF, nF, Oc, R_BOSS, (-dirF[0], -dirF[1]))   # FP enters boss
t_o_cf = add(Oc, unit(Oc, CF), R_BOSS)               # boss / front flank
# concave fillet front flank / small end
PFc = circle_circle(CF, ARM_FRONT_R - F_SMALL, Sc, R_SMALL + F_SMALL, dS)
t_f_fil = add(CF, unit(CF, PFc), ARM_FRONT_R)
t_s_f = add(Sc, unit(Sc, PFc), R_SMALL)
# concave fillet back flank / small end
PBc = circle_circle(CB, ARM_BACK_R - F_SMALL, Sc, R_SMALL + F_SMALL, dS)
t_cb_f = add(CB, unit(CB, PBc), ARM_BACK_R)
t_s_b = add(Sc, unit(Sc, PBc), R_SMALL)
t_o_cb = add(Oc, unit(Oc, CB), R_BOSS)               # boss / back flank
t_o_b1 = add(Oc, nB1, R_BOSS)
t_b_b1 = add(Bc, nB1, R_LOW_END)


def outline_A(z0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .moveTo(*t_b_f).lineTo(*i_f1)
            .threePointArc(arc_mid(Oc, R_BOSS, i_f1, t_o_cf, True), t_o_cf)
            .threePointArc(arc_mid(CF, ARM_FRONT_R, t_o_cf, t_f_fil, False), t_f_fil)
            .threePointArc(arc_mid(PFc, F_SMALL, t_f_fil, t_s_f, False), t_s_f)
            .threePointArc(arc_mid(Sc, R_SMALL, t_s_f, t_s_b, True), t_s_b)
            .threePointArc(arc_mid(PBc, F_SMALL, t_s_b, t_cb_f, False), t_cb_f)
            .threePointArc(arc_mid(CB, ARM_BACK_R, t_cb_f, t_o_cb, False), t_o_cb)
            .threePointArc(arc_mid(Oc, R_BOSS, t_o_cb, t_o_b1, True), t_o_b1)
            .lineTo(*t_b_b1)
            .threePointArc(arc_mid(Bc, R_LOW_END, t_b_b1, t_b_f, True), t_b_f)
            .close())


# ---------------- layer A : lower tine + hub + small arm -----------
layerA = outline_A(Z_BOT).extrude(Z_MID - Z_BOT)

# ---------------- layer B : upper tine ---------------------------
# upper tine front: flat tangent to the big end, blending into FP
nU = (math.cos(math.radians(UP_FRONT_DIR - 90.0)), math.sin(math.radians(UP_FRONT_DIR - 90.0)))
cU = dot(nU, Bc) + R_UP_END
t_ul = add(Bc, nU, R_UP_END)
detU = nU[0] * nF[1] - nU[1] * nF[0]
P_x = ((cU * nF[1] - nU[1] * cF) / detU, (nU[0] * cF - nF[0] * cU) / detU)
core_up = [Bc, t_ul, P_x, i_f1, Oc, t_o_b1, t_b_b1]
skB = (cq.Sketch()
       .polygon(closed(core_up))
       .push([Bc]).circle(R_UP_END)
       .reset().push([Oc]).circle(R_BOSS)
       .reset().clean())
skB = skB.vertices(near(P_x)).fillet(F_WAIST).reset()
# back: flank B1 (shared with the lower body) blended into the big end
pwb = line_circle(cB1, nB1, Bc, R_UP_END, (OX - BX, OY - BY))
skB = skB.vertices(near(pwb)).fillet(F_WAIST_B).reset()
layerB = slab(skB, Z_MID, Z_UP_TOP)

# ---------------- layer C : boss top -----------------------------
layerC = (cq.Workplane("XY").workplane(offset=Z_UP_TOP)
          .center(*Oc).circle(R_BOSS).extrude(Z_TOP - Z_UP_TOP))

# ---------------- slot between the tines -------------------------
BIG = 300.0
slot = (cq.Workplane("XY").workplane(offset=Z_TINE_TOP)
        .polyline(closed([frame(WALL_C - BIG, -BIG), frame(WALL_C + BIG, BIG),
                          frame(-BIG, BIG), frame(-BIG, -BIG)]))
        .close().extrude(Z_MID - Z_TINE_TOP))
layerA = layerA.cut(slot)


def wall_end(c_line, n_line):
    """XY point where the slot wall meets the line n.x = c"""
    p0, p1 = -200.0, 200.0
    f = lambda p: dot(n_line, frame(WALL_C + p, p)) - c_line
    for _ in range(80):
        pm = 0.5 * (p0 + p1)
        if f(p0) * f(pm) <= 0:
            p1 = pm
        else:
            p0 = pm
    return frame(WALL_C + p0, p0)


z_wall = 0.5 * (Z_TINE_TOP + Z_MID)
for (cl, nl, rr) in ((cB1, nB1, F_WALL_BACK), (cF, nF, F_WALL_FRONT)):
    pe = wall_end(cl, nl)
    try:
        layerA = layerA.edges(cq.selectors.NearestToPointSelector(
            (pe[0], pe[1], z_wall))).fillet(rr)
    except Exception:
        pass

# ---------------- inclined cut under the small arm ---------------
plane = cq.Plane(origin=(BX - BIG * nx, BY - BIG * ny, 0),
                 xDir=(ux, uy, 0), normal=(nx, ny, 0))
run = (CH_A1 - CH_A0) / Z_ARM_BOT
chamfer_cut = (cq.Workplane(plane)
               .polyline(closed([(CH_A0 - 2.0 * run, -2.0), (CH_A1, Z_ARM_BOT),
                                 (BIG, Z_ARM_BOT), (BIG, -2.0)]))
               .close().extrude(2 * BIG))
layerA = layerA.cut(chamfer_cut)

body = layerA.union(layerB).union(layerC)


# ---------------- fillets boss / tops ------------------------------
# concave blend between the boss wall and the faces it rises from, made
# as a revolved fillet ring clipped to the footprint of the lower layer
def fillet_ring(z, rf, a0, a1, footprint):
    inner = R_BOSS - 1.0 * K
    below = 0.3 * K
    c45 = math.cos(math.radians(45.0))
    prof = (cq.Workplane("XZ")
            .moveTo(inner, z - below)
            .lineTo(R_BOSS + rf, z - below)
            .lineTo(R_BOSS + rf, z)
            .threePointArc((R_BOSS + rf - rf * c45, z + rf - rf * c45),
                           (R_BOSS, z + rf))
            .lineTo(inner, z + rf)
            .close())
    span = (a1 - a0) % 360.0
    ring = prof.revolve(span, (0, 0, 0), (0, 1, 0))
    ring = ring.rotate((0, 0, 0), (0, 0, 1), a0).translate((OX, OY, 0))
    return ring.intersect(footprint)


def deg(p):
    return math.degrees(ang(Oc, p))


foot_A = outline_A(Z_MID - 1.0 * K).extrude(F_BOSS_ARM + 2.0 * K)
ring_arm = fillet_ring(Z_MID, F_BOSS_ARM, deg(t_o_cf), deg(t_o_cb), foot_A)
body = body.union(ring_arm)

foot_B = slab(skB, Z_UP_TOP - 1.0 * K, Z_UP_TOP + F_BOSS_UP + 1.0 * K)
ring_up = fillet_ring(Z_UP_TOP, F_BOSS_UP, deg(t_o_b1), deg(i_f1), foot_B)
body = body.union(ring_up)


# ---------------- holes -----------------------------------------
def cyl(c, r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(*c).circle(r).extrude(z1 - z0))


def cone(c, r0, z0, r1, z1):
    return cq.Workplane("XY").add(
        cq.Solid.makeCone(r0, r1, z1 - z0, pnt=cq.Vector(c[0], c[1], z0)))


body = body.cut(cyl(Bc, R_HOLE, Z_BOT - 1, Z_TOP + 1))
body = body.cut(cyl(Bc, R_CBORE, Z_UP_TOP - CBORE_DEPTH, Z_TOP + 1))
body = body.cut(cone(Bc, R_HOLE, Z_TINE_TOP - (R_CSK_LOW - R_HOLE),
                     R_CSK_LOW + 0.5, Z_TINE_TOP + 0.5))
body = body.cut(cyl(Oc, R_HOLE, Z_BOT - 1, Z_TOP + 1))
body = body.cut(cyl(Sc, R_HOLE_SMALL, Z_BOT - 1, Z_TOP + 1))

# rounded entry of the boss hole
hole_edges = [e for e in body.val().Edges()
              if e.geomType() == "CIRCLE" and abs(e.radius() - R_HOLE) < 1e-6
              and abs(e.Center().z - Z_TOP) < 1e-6]
try:
    body = body.newObject(hole_edges).fillet(F_BOSS_HOLE)
except Exception:
    body = body.cut(cone(Oc, R_HOLE, Z_TOP - F_BOSS_HOLE,
                         R_HOLE + F_BOSS_HOLE + 0.5, Z_TOP + 0.5))

result = body
